import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# A 1-7/8" ball on a 1/2" x 5/8" square shank (inch design, expressed in mm).
IN = 25.4
BALL_D = 1.875 * IN        # sphere diameter
FLAT_DROP = 0.75 * IN      # flat cut distance below the sphere centre
BAR_X = 0.5 * IN           # shank width along X
BAR_Y = 0.625 * IN         # shank width along Y
BAR_L = 1.25 * IN          # shank length below the flat
HOLE_D = 5.0 / 32.0 * IN   # cross-hole diameter (drilled along X)
HOLE_Z1 = 15.0 / 32.0 * IN # first hole, distance below the flat
HOLE_Z2 = 15.0 / 16.0 * IN # second hole, distance below the flat

R = BALL_D / 2.0
OVERLAP = 1.5              # shank overlap into the ball for a clean union

# ---------------- ball ----------------
# Plain sphere with a vertical polar axis.  Its seam meridian is turned to the
# (-X, +Y) side, facing away from the default camera -- purely cosmetic.
SEAM_DIR = cq.Vector(-1, 1, 0).normalized()
sphere = cq.Solid.makeSphere(R, cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), -90, 90, 360)
sphere = sphere.moved(cq.Location(cq.Plane(origin=(0, 0, 0), xDir=SEAM_DIR, normal=(0, 0, 1))))
ball = cq.Workplane("XY").add(sphere)

# flat underside
cutter = cq.Workplane("XY").box(4 * R, 4 * R, 2 * R).translate((0, 0, -FLAT_DROP - R))
ball = ball.cut(cutter)

# ---------------- square bar ----------------
bar = (cq.Workplane("XY").workplane(offset=-FLAT_DROP - BAR_L)
       .rect(BAR_X, BAR_Y).extrude(BAR_L + OVERLAP))   # small overlap into the ball
part = ball.union(bar)

# ---------------- cross holes (along X) ----------------
for hz in (HOLE_Z1, HOLE_Z2):
    # through hole along X; the bore's seam line lies on its top (+Z) side
    cyl = cq.Solid.makeCylinder(HOLE_D / 2.0, 2 * BAR_X,
                                cq.Vector(-BAR_X, 0, -FLAT_DROP - hz), cq.Vector(1, 0, 0))
    part = part.cut(cq.Workplane("XY").add(cyl))

result = part

VIEW = {"azimuth": 45, "elevation": 26}
